import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0        # length along Y
W = 48.0         # width along X
H = 12.0         # overall height (Z)
R_CORNER = 2.0   # vertical corner radius
R_TOP = 1.9      # fillet on top outer edges
T_WALL = 1.5     # side wall thickness
T_TOP = 2.0      # top plate thickness

HOLE_DX = 4.8    # hole centre inset from X sides
HOLE_DY = 5.0    # hole centre inset from Y ends
HOLE_D = 2.0     # through hole
PILOT_D = 2.6    # wider bore from below in the bosses
PILOT_H = 2.5
CSK_D = 4.4      # shallow countersink: outer diameter
CSK_MID_D = 3.4  # ring where the countersink steepens
CSK_MID_Z = 0.1  # depth of that ring
CSK_Z = 0.22     # depth at which the through hole starts

BOSS_D = 9.0     # screw bosses under the top plate
BOSS_H = 2.3

RIB_R = 2.35     # rounded ribs on inner +X wall
RIB_OFF = 0.85   # rib axis offset from the inner wall face
RIB_Y = (-39.7, -24.7, -9.7)

SLOT_H = 0.7     # small notches in the -X wall bottom edge: (centre Y, width)
SLOTS = [(-41.5, 5.0), (-30.1, 3.0), (-18.7, 3.0), (-8.6, 3.0),
         (8.6, 3.0), (18.7, 3.0), (30.1, 3.0), (41.5, 5.0)]

NOTCH_X0 = -9.2  # cable notch at -Y end (X range)
NOTCH_X1 = -3.0
NOTCH_H = 4.1

TEXT = "Lyric"
TEXT_SIZE = 16.7
TEXT_DEPTH = 0.8
TEXT_DX = 0.5    # text centre offset in X
DOT_D = 2.6      # round dot of the "i"

# ---------------- body ----------------
outer = (cq.Workplane("XY").rect(W, L).extrude(H)
         .edges("|Z").fillet(R_CORNER)
         .faces(">Z").edges().fillet(R_TOP))

# hollow underside (open cavity)
CAV_H = H - T_TOP
cav = (cq.Workplane("XY").rect(W - 2 * T_WALL, L - 2 * T_WALL).extrude(CAV_H)
       .edges("|Z").fillet(max(R_CORNER - T_WALL, 0.3)))
body = outer.cut(cav)

# screw bosses hanging from the top plate at the four corners
pts = [(sx * (W / 2 - HOLE_DX), sy * (L / 2 - HOLE_DY)) for sx in (-1, 1) for sy in (-1, 1)]
bosses = (cq.Workplane("XY").workplane(offset=CAV_H - BOSS_H)
          .pushPoints(pts).circle(BOSS_D / 2).extrude(BOSS_H + 0.5))
body = body.union(bosses.intersect(outer))

# half-round ribs on the inner face of the +X wall
for y in RIB_Y:
    rib = (cq.Workplane("XY").center(W / 2 - T_WALL - RIB_OFF, y)
           .circle(RIB_R).extrude(CAV_H + 0.2))
    body = body.union(rib.intersect(outer))

# shallow countersunk screw holes, revolved cutter (r, z) profile
prof = [(0, H + 1), (CSK_D / 2 + 1, H + 1), (CSK_D / 2 + 1, H),
        (CSK_D / 2, H), (CSK_MID_D / 2, H - CSK_MID_Z),
        (HOLE_D / 2, H - CSK_Z), (HOLE_D / 2, -1), (0, -1)]
for (px, py) in pts:
    cutter = (cq.Workplane("XZ").polyline(prof).close()
              .revolve(360, (0, 0, 0), (0, 1, 0))
              .translate((px, py, 0)))
    body = body.cut(cutter)
    pilot = (cq.Workplane("XY").workplane(offset=-1).center(px, py)
             .circle(PILOT_D / 2).extrude(CAV_H - BOSS_H + PILOT_H + 1))
    body = body.cut(pilot)

# cable notch at the -Y end
notch = (cq.Workplane("XY")
         .center((NOTCH_X0 + NOTCH_X1) / 2, -L / 2)
         .rect(NOTCH_X1 - NOTCH_X0, 4 * T_WALL).extrude(NOTCH_H))
body = body.cut(notch)

# small notches along the bottom edge of the -X wall
for (y, w) in SLOTS:
    s = (cq.Workplane("XY").center(-W / 2, y)
         .rect(4 * T_WALL, w).extrude(SLOT_H))
    body = body.cut(s)

# engraved logo on the top face, reading along +Y (letter tops toward -X)
def logo_cutter():
    tp = cq.Plane(origin=(TEXT_DX, 0, H + 0.1), xDir=(0, 1, 0), normal=(0, 0, 1))
    flat = cq.Compound.makeText(TEXT, TEXT_SIZE, 0, kind="bold",
                                halign="center", valign="center", position=tp)
    faces = list(flat.Faces())
    amax = max(f.Area() for f in faces)
    solids = []
    for f in faces:
        if f.Area() < 0.2 * amax:      # round the dot of the "i"
            f = cq.Face.makeFromWires(
                cq.Wire.makeCircle(DOT_D / 2, f.Center(), cq.Vector(0, 0, 1)))
        solids.append(cq.Solid.extrudeLinear(f, cq.Vector(0, 0, -(TEXT_DEPTH + 0.1))))
    return cq.Compound.makeCompound(solids)


try:
    body = body.cut(logo_cutter())
except Exception:
    try:
        tp = cq.Plane(origin=(TEXT_DX, 0, H), xDir=(0, 1, 0), normal=(0, 0, 1))
        txt = cq.Workplane(tp).text(TEXT, TEXT_SIZE, -TEXT_DEPTH, combine=False,
                                    kind="bold", halign="center", valign="center")
        body = body.cut(txt)
    except Exception:
        pass

result = body
